import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
N_TEETH = 32              # number of belt grooves (GT2 style, 2 mm pitch)
R_TOOTH = 9.93            # outside radius of the toothed section (lands)
R_FLANGE = 10.68          # flange outer radius
T_RIM = 0.86              # cylindrical rim thickness of each flange
H_CONE = 0.76             # height of the 45 deg conical inner face of each flange
L_TEETH = 12.15           # length of the toothed section between flanges

# GT2 groove, built from tangent arcs
GROOVE_R = 0.61           # radius of the round groove bottom
GROOVE_C = 0.19           # depth of the groove-bottom arc centre below the OD
LAND_FILLET = 0.15        # tangent blend radius between groove and land

BORE_R = 3.0              # D-bore radius
BORE_FLAT = 2.5           # distance from axis to the D flat (flat on -X side)

SEAM_ANGLE = 135.0        # where the revolve seams of the flanges sit (back side)
LEDGE = 0.03              # tiny flat ring where the flange cone meets the tooth OD

H_TOTAL = 2 * (T_RIM + H_CONE) + L_TEETH
Z_T0 = T_RIM + H_CONE             # bottom of toothed section
Z_T1 = Z_T0 + L_TEETH             # top of toothed section


def rot(p, a):
    c, s = math.cos(a), math.sin(a)
    return (p[0] * c - p[1] * s, p[0] * s + p[1] * c)


def unit(v):
    l = math.hypot(v[0], v[1])
    return (v[0] / l, v[1] / l)


def tooth_profile():
    """Closed 2D wire of the toothed section: lands on R_TOOTH, round groove
    bottoms and tangent fillet blends - all true arcs. Groove i is centred on
    angle i*pitch (one groove points along +X)."""
    c = R_TOOTH - GROOVE_C                     # groove-centre radius
    rf = R_TOOTH - LAND_FILLET                 # fillet-centre radius
    d = GROOVE_R + LAND_FILLET
    alpha = math.acos((rf ** 2 + c ** 2 - d ** 2) / (2 * rf * c))
    G = (c, 0.0)
    F = (rf * math.cos(alpha), rf * math.sin(alpha))
    T1 = (R_TOOTH * math.cos(alpha), R_TOOTH * math.sin(alpha))   # land/fillet
    u = unit((F[0] - G[0], F[1] - G[1]))
    T2 = (G[0] + GROOVE_R * u[0], G[1] + GROOVE_R * u[1])          # fillet/groove
    m = unit((math.cos(alpha) - u[0], math.sin(alpha) - u[1]))
    FM = (F[0] + LAND_FILLET * m[0], F[1] + LAND_FILLET * m[1])    # fillet mid
    B = (c - GROOVE_R, 0.0)                                        # groove bottom

    def mir(p):
        return (p[0], -p[1])

    pitch = 2 * math.pi / N_TEETH
    wp = cq.Workplane("XY").workplane(offset=Z_T0).moveTo(*mir(T1))
    for i in range(N_TEETH):
        a = i * pitch
        wp = (wp.threePointArc(rot(mir(FM), a), rot(mir(T2), a))
                .threePointArc(rot(B, a), rot(T2, a))
                .threePointArc(rot(FM, a), rot(T1, a))
                .threePointArc(rot((R_TOOTH, 0.0), a + pitch / 2),
                               rot(mir(T1), a + pitch)))
    return wp.close()


def flange(top):
    """Revolved flange: cylindrical rim plus a 45 deg cone down to the tooth OD."""
    prof = (cq.Workplane("XZ")
            .moveTo(0, 0)
            .lineTo(R_FLANGE, 0)
            .lineTo(R_FLANGE, T_RIM)
            .lineTo(R_TOOTH + LEDGE, T_RIM + H_CONE)
            .lineTo(0, T_RIM + H_CONE)
            .close())
    f = prof.revolve(360, (0, 0, 0), (0, 1, 0))
    f = f.rotate((0, 0, 0), (0, 0, 1), SEAM_ANGLE)
    if top:
        f = f.mirror("XY").translate((0, 0, H_TOTAL))
    return f


# toothed body (grooved section between the flanges)
body = tooth_profile().extrude(L_TEETH)

part = flange(False).union(body).union(flange(True))

# D bore through the whole pulley
half = math.sqrt(BORE_R ** 2 - BORE_FLAT ** 2)
bore = (cq.Workplane("XY")
        .moveTo(-BORE_FLAT, -half)
        .threePointArc((BORE_R, 0), (-BORE_FLAT, half))
        .close()
        .extrude(H_TOTAL))
result = part.cut(bore)

VIEW = {"azimuth": 45, "elevation": 26}
